import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FLANGE_R = 30.0          # base flange radius
FLANGE_T = 3.5          # flange thickness
BODY_R = 27.05           # outer radius of the four lobes
BODY_H = 16.85           # lobe body height above flange
ARM_HALF_W = 12.75       # half width of each cross arm (lobe)
CROSS_ROT = -5.5         # rotation of the lobe cross about Z (deg)
NOTCH_IN_FILLET = 3.0    # concave notch corner fillet
NOTCH_OUT_FILLET = 2.2   # convex lobe corner fillet

BOSS_R = 17.75           # raised central boss radius
BOSS_H = 4.35            # boss height above lobe top
BOSS_FILLET = 2.5        # rounded top edge of boss
RECESS_R = 12.25         # counterbore recess in boss top
RECESS_D = 1.7           # recess depth
HOLE_R = 5.85            # through hole radius

SPLINE_N = 15            # number of spline teeth (underside bore)
SPLINE_R_MAJ = 11.3     # spline major radius
SPLINE_R_MIN = 9.9      # spline minor radius
SPLINE_DEPTH = 16.0      # spline bore depth from bottom
SPLINE_PHASE = 6.5       # angle of first tooth-space peak (deg)

Z_TOP = FLANGE_T + BODY_H

# ---------------- flange ----------------
flange = cq.Workplane("XY").circle(FLANGE_R).extrude(FLANGE_T)

# ---------------- lobed body (circle cut by a cross) ----------------
big = 2.5 * BODY_R
cross = (
    cq.Workplane("XY")
    .rect(2 * ARM_HALF_W, big)
    .extrude(BODY_H)
    .union(cq.Workplane("XY").rect(big, 2 * ARM_HALF_W).extrude(BODY_H))
)
disk = cq.Workplane("XY").circle(BODY_R).extrude(BODY_H)
body = disk.intersect(cross)

# fillet vertical edges: concave inner corners vs convex outer corners
inner_r = math.sqrt(2) * ARM_HALF_W


class _RadSel(cq.Selector):
    def __init__(self, rmin, rmax):
        self.rmin, self.rmax = rmin, rmax

    def filter(self, objs):
        out = []
        for e in objs:
            c = e.Center()
            r = math.hypot(c.x, c.y)
            if self.rmin <= r <= self.rmax:
                out.append(e)
        return out


body = body.edges("|Z").edges(_RadSel(inner_r - 0.5, inner_r + 0.5)).fillet(NOTCH_IN_FILLET)
body = body.edges("|Z").edges(_RadSel(BODY_R - 0.5, BODY_R + 0.5)).fillet(NOTCH_OUT_FILLET)
body = body.rotate((0, 0, 0), (0, 0, 1), CROSS_ROT).translate((0, 0, FLANGE_T))

# ---------------- central boss ----------------
boss = (
    cq.Workplane("XY")
    .workplane(offset=Z_TOP)
    .circle(BOSS_R)
    .extrude(BOSS_H)
    .faces(">Z")
    .edges()
    .fillet(BOSS_FILLET)
)

part = flange.union(body).union(boss)

# recess on boss top
z_boss_top = Z_TOP + BOSS_H
recess = (
    cq.Workplane("XY")
    .workplane(offset=z_boss_top - RECESS_D)
    .circle(RECESS_R)
    .extrude(RECESS_D + 1)
)
part = part.cut(recess)

# through hole
hole = cq.Workplane("XY").workplane(offset=-1).circle(HOLE_R).extrude(z_boss_top + 2)
part = part.cut(hole)

# ---------------- splined bore from underside ----------------
def spline_profile(n, r_maj, r_min):
    r_mid = 0.5 * (r_maj + r_min)
    step = 2 * math.pi / n

    def pt(r, a):
        return (r * math.cos(a), r * math.sin(a))

    ph = math.radians(SPLINE_PHASE)
    start = pt(r_mid, ph - step / 4)
    wp = cq.Workplane("XY").workplane(offset=-1).moveTo(*start)
    for k in range(n):
        a0 = ph + k * step
        wp = wp.threePointArc(pt(r_maj, a0), pt(r_mid, a0 + step / 4))
        wp = wp.threePointArc(pt(r_min, a0 + step / 2), pt(r_mid, a0 + 3 * step / 4))
    return wp.close()


spline = spline_profile(SPLINE_N, SPLINE_R_MAJ, SPLINE_R_MIN).extrude(SPLINE_DEPTH + 1)
part = part.cut(spline)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
